import math
import cadquery as cq

# =====================================================================
#  Thin-walled "beak" sleeve:
#    vertical tube (radius R)  +  equal-radius branch pipe tilted down
#    toward +Y, squeezed by a top-view wedge into a beak, hollowed to a
#    constant wall, then trimmed by a side (YZ) profile, a crescent cut
#    and a front (XZ) spike profile.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
R = 20.0            # radius of the vertical tube and of the branch pipe
T = 0.075 * R       # wall thickness of the vertical tube
H = 3.6 * R         # raw tube height before trimming

# branch pipe (same radius) : axis in the YZ plane, tilted down toward +Y
BR_Z0 = 1.881 * R                 # height where the branch axis meets the tube axis
BR_SLOPE = 0.32                   # dZ/dY of the branch axis (falls toward the beak)
BR_ANG = math.atan(BR_SLOPE)

# wedge (top view) that squeezes the branch into a beak
TIP_Y = 3.02 * R                  # apex of the squeezing wedge (top view), just past the beak tip
WEDGE_PT = (0.987 * R, 0.69 * R)  # a point on the wedge side line

# hollow of the branch / beak, measured in vertical Y-sections
BR_IN_A = 0.88 * R                # inner half-width  (side walls ~0.12R)
BR_IN_B = 0.99 * R                # inner half-height (roof / keel ~0.06R)
TW = 0.075 * R                    # wall thickness of the wedge (beak) flanks

# front notch (side view circle, cut along X)
NOTCH_C = (-0.507 * R, 1.007 * R)
NOTCH_R = 0.628 * R
BAND_H = 0.507 * R                # band height at the front
FRONT_CUT_Y = -0.315 * R          # where the front opening meets the outer wall (side view)
FRONT_DRAFT = math.radians(25.0)  # draft of the front opening's side faces (top view)
FRONT_Z0 = 1.55 * R               # the drafted front opening starts just above the notch
KEEP_Y = -0.50 * R                # side-profile line hidden behind the drafted cut

# side-view top edge arc (circle through measured points)
TOP_CY = -0.4582 * R
TOP_CZ = 3.5704 * R
TOP_RR = 1.4196 * R
TOP_YA = KEEP_Y                   # start of the top arc (front)
TOP_YB = 0.686 * R                # arc end: kink where the spike flank starts (side view)
# side-view flank of the spike (Y, Z in units of R), from the kink up past the cusp
SPIKE_SIDE = [(0.78, 2.79), (0.855, 2.875), (0.906, 2.99), (0.926, 3.15), (0.958, 3.315),
              (0.99, 3.40), (1.02, 3.50)]

# front-view spike: two concave circular flanks meeting in a cusp at X=0
SPIKE_CX = 2.1394 * R             # |X| of flank circle centre
SPIKE_CZ = 4.9931 * R             # Z of flank circle centre
SPIKE_RF = 2.6555 * R             # flank circle radius
SPIKE_XEND = 0.95 * R             # flank arcs run out to this |X|

# crescent cut seen from the side (Y, Z) in units of R, from beak tip round to horn tip
CRESCENT = [(3.30, 2.20), (3.10, 2.04), (3.00, 2.00), (2.90, 1.99), (2.703, 2.0), (2.228, 2.13),
            (1.774, 2.20), (1.452, 2.195), (1.129, 2.136), (0.903, 2.007), (0.757, 1.846),
            (0.693, 1.683), (0.71, 1.458), (0.78, 1.212), (0.973, 0.954), (1.297, 0.695),
            (1.62, 0.505), (1.942, 0.315), (2.266, 0.13), (2.40, 0.07), (2.50, 0.025), (2.70, -0.08)]

BIG = 10 * R
NC = dict(clean=True)


def s(p):
    return (p[0] * R, p[1] * R)


# ---------------- helpers ----------------
def tube_solid(r, z0, z1):
    # periodic seam of the cylindrical face put at the front-left (theta = 225 deg),
    # where only the low band survives and the seam sits on most silhouettes
    sd = math.sqrt(0.5)
    pl = cq.Plane(origin=(0, 0, z0), xDir=(-sd, -sd, 0), normal=(0, 0, 1))
    return cq.Workplane(pl).circle(r).extrude(z1 - z0)


def zc(y):
    """height of the branch axis at a given Y"""
    return BR_Z0 - BR_SLOPE * y


def ysection(y, a, b):
    """ellipse in the vertical plane Y=y centred on the branch axis"""
    pl = cq.Plane(origin=(0, y, zc(y)), xDir=(1, 0, 0), normal=(0, 1, 0))
    return cq.Workplane(pl).ellipse(a, b).val()


def branch_solid(a, b, wedge_off):
    """tilted pipe with constant vertical Y-section (a x b), starting at the tube axis
    plane Y=0, squeezed by a vertical top-view wedge into a beak"""
    y1 = 4.0 * R
    pipe = cq.Workplane("XY").add(cq.Solid.makeLoft([ysection(0.0, a, b), ysection(y1, a, b)], True))
    wx, wy = WEDGE_PT
    k = wx / (TIP_Y - wy)           # half-width per unit Y
    yb = -2 * R
    tip = TIP_Y - wedge_off / math.sin(math.atan(k))
    xb = k * (tip - yb)
    wedge = (cq.Workplane("XY").workplane(offset=-2 * R)
             .polyline([(-xb, yb), (xb, yb), (0, tip)]).close()
             .extrude(8 * R))
    return pipe.intersect(wedge, **NC)


# ---------------- thin-walled body ----------------
BR_B = R / math.cos(BR_ANG)       # half-height of the branch Y-section (circular pipe)
outer = tube_solid(R, -0.5 * R, H).union(branch_solid(R, BR_B, 0.0), **NC)
inner = tube_solid(R - T, -R, H + R).union(branch_solid(BR_IN_A, BR_IN_B, TW), **NC)
shell = outer.cut(inner, **NC)


# ---------------- side profile (kept region, extruded along X) ----------------
def top_z(y):
    return TOP_CZ - math.sqrt(TOP_RR**2 - (y - TOP_CY)**2)


def spike_z(x):
    return SPIKE_CZ - math.sqrt(SPIKE_RF**2 - (SPIKE_CX - abs(x))**2)


dy0 = math.sqrt(NOTCH_R**2 - (BAND_H - NOTCH_C[1])**2)
ny0 = NOTCH_C[0] - dy0                                   # notch start on the band top
ang0 = math.atan2(BAND_H - NOTCH_C[1], -dy0)
ztop_notch = NOTCH_C[1] + math.sqrt(NOTCH_R**2 - (KEEP_Y - NOTCH_C[0])**2)
a_end = math.atan2(ztop_notch - NOTCH_C[1], KEEP_Y - NOTCH_C[0])
a_mid = 0.5 * (ang0 + a_end)
notch_mid = (NOTCH_C[0] + NOTCH_R * math.cos(a_mid), NOTCH_C[1] + NOTCH_R * math.sin(a_mid))
ym = 0.5 * (TOP_YA + TOP_YB)

keep_side = (cq.Workplane("YZ")
             .moveTo(-2 * R, -R)
             .lineTo(-2 * R, BAND_H)
             .lineTo(ny0, BAND_H)
             .threePointArc(notch_mid, (KEEP_Y, ztop_notch))
             .lineTo(TOP_YA, top_z(TOP_YA))
             .threePointArc((ym, top_z(ym)), (TOP_YB, top_z(TOP_YB)))
             .spline([s(p) for p in SPIKE_SIDE], includeCurrent=True)
             .lineTo(SPIKE_SIDE[-1][0] * R, 4.5 * R)
             .lineTo(5 * R, 4.5 * R)
             .lineTo(5 * R, -R)
             .close()
             .extrude(BIG, both=True))

# ---------------- crescent cut (through all, along X) ----------------
c_pts = [s(p) for p in CRESCENT]
crescent = (cq.Workplane("YZ")
            .moveTo(*c_pts[0])
            .spline(c_pts[1:], includeCurrent=True)
            .lineTo(6 * R, -1.0 * R)
            .lineTo(6 * R, 2.5 * R)
            .lineTo(c_pts[0][0], 2.5 * R)
            .close()
            .extrude(BIG, both=True))

# ---------------- front profile (cut along Y): pointed spike ----------------
xm = 0.5 * SPIKE_XEND
spike_cut = (cq.Workplane("XZ")
             .moveTo(-SPIKE_XEND, spike_z(SPIKE_XEND))
             .threePointArc((-xm, spike_z(xm)), (0, spike_z(0)))
             .threePointArc((xm, spike_z(xm)), (SPIKE_XEND, spike_z(SPIKE_XEND)))
             .lineTo(SPIKE_XEND, 5 * R)
             .lineTo(-SPIKE_XEND, 5 * R)
             .close()
             .extrude(BIG, both=True))

# ---------------- drafted front opening (top-view trapezoid, vertical faces) ----------------
xo = math.sqrt(R**2 - FRONT_CUT_Y**2)            # |X| of the opening edge on the outer wall


def front_w(y):
    return xo - (y - FRONT_CUT_Y) * math.tan(FRONT_DRAFT)


front_cut = (cq.Workplane("XY").workplane(offset=FRONT_Z0)
             .polyline([(-front_w(-1.5 * R), -1.5 * R), (front_w(-1.5 * R), -1.5 * R),
                        (front_w(0), 0), (-front_w(0), 0)]).close()
             .extrude(3 * R))

floor_box = cq.Workplane("XY").box(20 * R, 20 * R, 10 * R, centered=(True, True, False))

result = (shell.cut(crescent, **NC)
          .intersect(keep_side, **NC)
          .cut(spike_cut, **NC)
          .cut(front_cut, **NC)
          .intersect(floor_box, **NC))
